import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 90.0          # overall length (Y)
W = 29.5          # overall width (X)
H = 6.7           # body height (Z)
R_CORNER = 2.5    # vertical corner radius of the body
F_TOP = 0.25      # small fillet on the top outer edge

# storage pocket (at the -Y end)
P_RIM_SIDE = 2.6      # rim width on the long sides
P_RIM_END = 2.9       # rim width at the -Y end
P_LEN = 52.9          # pocket length along Y
P_DEPTH = 3.5         # pocket depth
P_R = 1.0             # pocket corner radius
P_FLOOR_F = 0.5       # fillet between pocket wall and floor

# stepped (counterbored) blind recess near the +Y end
CB_Y_FROM_END = 17.2  # centre distance from the +Y end
CB_D1 = 17.4          # large shallow diameter
CB_H1 = 2.55          # depth of the large step
CB_D2 = 11.3          # small deep diameter
CB_H2 = 3.05          # additional depth of the small step

# two small blind holes at the +Y corners
SH_D = 4.1
SH_OFF = 5.0          # offset from the side and end faces
SH_DEPTH = 3.5

# raised lettering
TXT = "THEORIES"
TXT_Y_FROM_END = 30.3  # centre distance from the +Y end
TXT_H = 4.15            # cap height of the letters
TXT_X = [-10.25, -7.1, -3.9, -0.66, 2.42, 5.05, 7.63, 10.74]  # letter centres (X)
TXT_SX = [0.72, 0.74, 0.85, 0.70, 0.79, 1.25, 0.87, 0.93]  # per-glyph squeeze
TXT_FONT_SIZE = 5.0
TXT_RAISE = 0.15
TXT_SLANT = 14.0       # italic slant (deg)

# L-shaped rail along the bottom of the -X side
RAIL_LEN = 64.2
RAIL_Y0 = 0.1          # centre of rail along Y
RAIL_OUT = 1.95        # how far the rail sticks out from the side
RAIL_T = 0.8           # thickness of the base strip
RAIL_LIP_W = 0.85      # lip width
RAIL_LIP_H = 1.9       # lip height

# ---------------- body ----------------
body = (
    cq.Workplane("XY")
    .rect(W, L)
    .extrude(H)
    .edges("|Z")
    .fillet(R_CORNER)
)
body = body.faces(">Z").edges().fillet(F_TOP)

# pocket
p_y1 = -L / 2 + P_RIM_END
p_y2 = p_y1 + P_LEN
p_w = W - 2 * P_RIM_SIDE
pocket = (
    cq.Workplane("XY")
    .workplane(offset=H - P_DEPTH)
    .center(0, (p_y1 + p_y2) / 2)
    .rect(p_w, P_LEN)
    .extrude(P_DEPTH + 1)
    .edges("|Z")
    .fillet(P_R)
    .faces("<Z")
    .edges()
    .fillet(P_FLOOR_F)
)
body = body.cut(pocket)

# counterbored blind recess
cb_y = L / 2 - CB_Y_FROM_END
cb1 = (
    cq.Workplane("XY")
    .workplane(offset=H - CB_H1)
    .center(0, cb_y)
    .circle(CB_D1 / 2)
    .extrude(CB_H1 + 1)
)
cb2 = (
    cq.Workplane("XY")
    .workplane(offset=H - CB_H1 - CB_H2)
    .center(0, cb_y)
    .circle(CB_D2 / 2)
    .extrude(CB_H2 + 0.5)
)
body = body.cut(cb1).cut(cb2)

# small blind holes
sh = (
    cq.Workplane("XY")
    .workplane(offset=H - SH_DEPTH)
    .pushPoints([(-W / 2 + SH_OFF, L / 2 - SH_OFF), (W / 2 - SH_OFF, L / 2 - SH_OFF)])
    .circle(SH_D / 2)
    .extrude(SH_DEPTH + 1)
)
body = body.cut(sh)

# soften the rims of the pocket and the holes (inner wires of the top face)
F_RIM = 0.25
solid = body.val()
top_face = body.faces(">Z").val()
rim_edges = [e for w in top_face.innerWires() for e in w.Edges()]
# rim of the small step of the counterbore
for e in solid.Edges():
    c = e.Center()
    if abs(c.z - (H - CB_H1)) < 1e-3 and e.geomType() == "CIRCLE":
        if abs(e.radius() - CB_D2 / 2) < 1e-3:
            rim_edges.append(e)
solid = solid.fillet(F_RIM, rim_edges)
body = cq.Workplane("XY").add(solid)

# rail (L profile) on the -X side, flush with the bottom
rail_profile = (
    cq.Workplane("XZ")
    .polyline(
        [
            (-W / 2 + 0.3, 0),
            (-W / 2 - RAIL_OUT, 0),
            (-W / 2 - RAIL_OUT, RAIL_LIP_H),
            (-W / 2 - RAIL_OUT + RAIL_LIP_W, RAIL_LIP_H),
            (-W / 2 - RAIL_OUT + RAIL_LIP_W, RAIL_T),
            (-W / 2 + 0.3, RAIL_T),
        ]
    )
    .close()
    .extrude(RAIL_LEN / 2, both=True)
    .translate((0, RAIL_Y0, 0))
)
body = body.union(rail_profile)

# raised lettering: bold font glyphs, squeezed, slanted and spaced one by one
def make_text():
    from OCP.gp import gp_GTrsf, gp_Mat, gp_XYZ
    from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform

    k = math.tan(math.radians(TXT_SLANT))
    y_mid = L / 2 - TXT_Y_FROM_END
    font = dict(font="DejaVu Sans", kind="bold", halign="left", valign="bottom")
    # cap height of the font, measured on a flat-topped capital
    cap = cq.Workplane("XY").text("H", TXT_FONT_SIZE, TXT_RAISE, combine=False, **font)
    cap = cap.val().BoundingBox(tolerance=1e-3)
    sy = TXT_H / (cap.ymax - max(cap.ymin, 0.0))
    glyphs = []
    for ch, xc, sx in zip(TXT, TXT_X, TXT_SX):
        g0 = cq.Workplane("XY").text(ch, TXT_FONT_SIZE, TXT_RAISE, combine=False, **font).val()
        bb = g0.BoundingBox(tolerance=1e-3)
        cx = (bb.xmin + bb.xmax) / 2
        m = gp_Mat(sx, k * sy, 0.0, 0.0, sy, 0.0, 0.0, 0.0, 1.0)
        tr = gp_GTrsf()
        tr.SetVectorialPart(m)
        tr.SetTranslationPart(
            gp_XYZ(-sx * cx - k * TXT_H / 2 + xc, y_mid - TXT_H / 2, H - 0.01)
        )
        glyphs.append(cq.Shape.cast(BRepBuilderAPI_GTransform(g0.wrapped, tr, True).Shape()))
    return cq.Compound.makeCompound(glyphs)


try:
    txt = make_text()
    body = body.union(cq.Workplane("XY").add(txt))
except Exception as e:  # lettering is cosmetic; keep the part if fonts fail
    print("text skipped:", e)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
